import math
import cadquery as cq
from OCP.Geom import Geom_BSplineCurve
from OCP.TColgp import TColgp_Array1OfPnt
from OCP.TColStd import TColStd_Array1OfReal, TColStd_Array1OfInteger
from OCP.gp import gp_Pnt
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge

# ---------------- driving dimensions (mm) ----------------
W = 100.0          # width along X
L = 240.0          # length along Y (front wall to back wall)
H = 45.0           # overall height
T = 2.5            # top plate thickness
DRAFT = 5.0        # outer wall draft (deg)
BEND_OUT = 7.5     # outer bend: tangent distance from the sharp corner
BEND_IN = 6.5      # inner bend: tangent distance from the sharp corner
WALL_IN = 5.8      # inner wall face, measured inward from outer bottom edge

# screw lugs at the four wall ends (profile measured from outer bottom edge)
LUG_LEN = 4.0      # lug length along X
LUG1_FACE, LUG1_TOP, LUG1_SLOPE_END, LUG1_BOT = 13.2, 35.2, 27.5, 19.8
LUG2_FACE, LUG2_TOP, LUG2_SLOPE_END = 13.7, 14.9, 6.3
PORT_D, PORT_DY, PORT_Z1, PORT_Z2 = 4.2, 9.2, 24.5, 4.7

# vertical screw bosses against the inner wall faces (sloped top)
BOSS_D, BOSS_DY, BOSS_ZB, BOSS_H, BOSS_HOLE_D = 9.0, 6.3, 0.0, 13.2, 3.0
BOSS_TOP_SLOPE = 45.0   # deg, top face rises toward the wall
BOSS_XS = {-1: (-32.5, 32.5), 1: (-32.5, 32.5)}   # X positions on the front (-1) and back (+1) wall

# top plate cut-outs
WIN_W, WIN_L, WIN_CX, WIN_CY = 50.3, 32.5, 0.0, 75.0       # large window
SQ_W, SQ_L, SQ_CX, SQ_CY = 22.0, 20.0, 0.0, -79.0          # small square opening
LED_SQ, LED_Y, LED_HOLE_D, LED_DX = 7.0, 48.0, 2.6, 7.5    # small square + 2 holes
LAB_W, LAB_L, LAB_CX, LAB_CY, LAB_R = 94.0, 69.5, 0.4, -18.0, 4.0
LAB_D, LAB_GROOVE_W, LAB_GROOVE_D, LAB_D_UNDER = 0.3, 0.9, 0.8, 0.4  # recess, perimeter groove, underside relief

# rectangular duct under the small square opening
BOX_X0, BOX_X1, BOX_Y0, BOX_Y1, BOX_ZB = -16.0, 18.0, -96.5, -56.0, 29.3
LEG_Y0, LEG_ZB = -64.6, 1.0

# post in front of the window
POST_X0, POST_X1 = -6.9, 8.7
POST_Y0, POST_Y1, POST_Y2, POST_ZSTEP = 29.3, 37.6, 43.3, 21.1
POST_PIN_X, POST_PIN_Z, POST_PIN_D, POST_PIN_DEPTH = -0.5, 14.0, 2.0, 5.0   # pin hole in the front face

# key-switch on the back wall
KEY_X, KEY_Z, KEY_REC_D, KEY_REC_DEPTH = 1.0, 20.0, 19.0, 3.0
KEY_SLOT_L, KEY_SLOT_W, KEY_SLOT_DX, KEY_SLOT_DZ = 12.5, 3.5, -3.0, 1.5
KBLK_X0, KBLK_X1, KBLK_Y0, KBLK_ZB = -6.2, 8.3, 99.0, 22.5

# snap tabs under the window
TAB_W, TAB_H, TAB_CH = 5.0, 3.8, 2.2
TAB_SPANS = {-1: (4.6, 2.5), 1: (8.4, 1.4)}   # per window edge: Y extent inside / outside the opening edge

# ---------------- helpers ----------------
tz = math.tan(math.radians(DRAFT))
zin = H - T
yw = L / 2.0 - WALL_IN       # |Y| of inner wall faces


def bspline_edge(pts, degree=2):
    """clamped uniform B-spline through control points -> single smooth edge"""
    n = len(pts)
    poles = TColgp_Array1OfPnt(1, n)
    for i, p in enumerate(pts):
        poles.SetValue(i + 1, gp_Pnt(*p))
    nk = n - degree + 1
    knots = TColStd_Array1OfReal(1, nk)
    mults = TColStd_Array1OfInteger(1, nk)
    for i in range(nk):
        knots.SetValue(i + 1, float(i))
        mults.SetValue(i + 1, degree + 1 if i in (0, nk - 1) else 1)
    return cq.Edge(BRepBuilderAPI_MakeEdge(Geom_BSplineCurve(poles, knots, mults, degree)).Edge())


def unit(a, b):
    d = (b[0] - a[0], b[1] - a[1])
    n = math.hypot(*d)
    return (d[0] / n, d[1] / n)


def box(x0, x1, y0, y1, z0, z1):
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False).translate((x0, y0, z0))


# ---------------- main body: U-shaped skin extruded along X ----------------
# outer skin = wall / bend / top / bend / wall as one smooth curve
cf = (-L / 2.0 + H * tz, H)
cb = (L / 2.0 - H * tz, H)
uf = unit(cf, (-L / 2.0, 0.0))
ub = unit(cb, (L / 2.0, 0.0))
outer_pts = [
    (-L / 2.0, 0.0),
    (cf[0] + 2 * BEND_OUT * uf[0], cf[1] + 2 * BEND_OUT * uf[1]),
    cf,
    (cf[0] + 2 * BEND_OUT, H),
    (cb[0] - 2 * BEND_OUT, H),
    cb,
    (cb[0] + 2 * BEND_OUT * ub[0], cb[1] + 2 * BEND_OUT * ub[1]),
    (L / 2.0, 0.0),
]
inner_pts = [
    (yw, 0.0), (yw, zin - 2 * BEND_IN), (yw, zin), (yw - 2 * BEND_IN, zin),
    (-yw + 2 * BEND_IN, zin), (-yw, zin), (-yw, zin - 2 * BEND_IN), (-yw, 0.0),
]
x0 = -W / 2.0
e_out = bspline_edge([(x0, y, z) for y, z in outer_pts])
e_in = bspline_edge([(x0, y, z) for y, z in inner_pts])
e_b1 = cq.Edge.makeLine(cq.Vector(x0, L / 2.0, 0), cq.Vector(x0, yw, 0))
e_b2 = cq.Edge.makeLine(cq.Vector(x0, -yw, 0), cq.Vector(x0, -L / 2.0, 0))
profile = cq.Face.makeFromWires(cq.Wire.assembleEdges([e_out, e_b1, e_in, e_b2]))
body = cq.Workplane("XY").add(cq.Solid.extrudeLinear(profile, cq.Vector(W, 0, 0)))


def wall_pt(sign, dy, z):
    return (sign * (L / 2.0 - dy), z)


# ---------------- end lugs with screw ports ----------------
for sgn in (-1, 1):
    up = [wall_pt(sgn, WALL_IN - 1.0, LUG1_BOT), wall_pt(sgn, LUG1_FACE, LUG1_BOT),
          wall_pt(sgn, LUG1_FACE, LUG1_SLOPE_END), wall_pt(sgn, WALL_IN, LUG1_TOP),
          wall_pt(sgn, WALL_IN - 1.0, LUG1_TOP)]
    lo = [wall_pt(sgn, WALL_IN - 1.0, 0.0), wall_pt(sgn, LUG2_FACE, 0.0),
          wall_pt(sgn, LUG2_FACE, LUG2_SLOPE_END), wall_pt(sgn, WALL_IN, LUG2_TOP),
          wall_pt(sgn, WALL_IN - 1.0, LUG2_TOP)]
    for xs in (-1, 1):
        xl = W / 2.0 - LUG_LEN if xs > 0 else -W / 2.0
        for poly in (up, lo):
            body = body.union(cq.Workplane("YZ", origin=(xl, 0, 0)).polyline(poly).close().extrude(LUG_LEN))

for sgn in (-1, 1):
    for zp in (PORT_Z1, PORT_Z2):
        yp = sgn * (L / 2.0 - PORT_DY)
        body = body.cut(cq.Workplane("YZ", origin=(-W / 2.0 - 1, 0, 0)).center(yp, zp)
                        .circle(PORT_D / 2.0).extrude(W + 2))

# ---------------- vertical bosses on the inner wall faces ----------------
for sgn in (-1, 1):
    for cx in BOSS_XS[sgn]:
        cy = sgn * (L / 2.0 - BOSS_DY)
        boss = cq.Workplane("XY", origin=(0, 0, BOSS_ZB)).center(cx, cy).circle(BOSS_D / 2.0).extrude(BOSS_H + BOSS_D)
        cutter = (
            cq.Workplane("XY").box(40, 40, 40).translate((0, 0, 20))
            .rotate((0, 0, 0), (1, 0, 0), sgn * BOSS_TOP_SLOPE)
            .translate((cx, cy, BOSS_H))
        )
        body = body.union(boss.cut(cutter))
        body = body.cut(cq.Workplane("XY", origin=(0, 0, BOSS_ZB - 1)).center(cx, cy).circle(BOSS_HOLE_D / 2).extrude(9))

# ---------------- label area ----------------
def lab_sketch(z, grow=0.0):
    return (cq.Workplane("XY", origin=(0, 0, z)).center(LAB_CX, LAB_CY)
            .sketch().rect(LAB_W + 2 * grow, LAB_L + 2 * grow).vertices().fillet(LAB_R + grow).finalize())


body = body.cut(lab_sketch(H - LAB_D).extrude(LAB_D + 1))
groove = lab_sketch(H - LAB_GROOVE_D).extrude(LAB_GROOVE_D + 1).cut(
    cq.Workplane("XY", origin=(0, 0, H - LAB_GROOVE_D - 1)).center(LAB_CX, LAB_CY)
    .sketch().rect(LAB_W - 2 * LAB_GROOVE_W, LAB_L - 2 * LAB_GROOVE_W).vertices()
    .fillet(LAB_R - LAB_GROOVE_W).finalize().extrude(LAB_GROOVE_D + 3))
body = body.cut(groove)
body = body.cut(lab_sketch(zin - 1.0).extrude(1.0 + LAB_D_UNDER))

# ---------------- duct under the small square opening ----------------
body = body.union(box(BOX_X0, BOX_X1, BOX_Y0, BOX_Y1, BOX_ZB, zin + 0.5))
body = body.union(box(BOX_X0, BOX_X1, LEG_Y0, BOX_Y1, LEG_ZB, zin + 0.5))
body = body.cut(cq.Workplane("XY", origin=(0, 0, BOX_ZB - 1.0)).center(SQ_CX, SQ_CY)
                .rect(SQ_W, SQ_L).extrude(H - BOX_ZB + 2.0))

# ---------------- post in front of the window ----------------
gus = (
    cq.Workplane("YZ", origin=(POST_X0, 0, 0))
    .polyline([(POST_Y0 + 0.5, zin + 0.2), (POST_Y0 - 3.0, zin + 0.2), (POST_Y0 + 0.5, zin - 3.5)]).close()
    .extrude(POST_X1 - POST_X0)
)
body = (body.union(box(POST_X0, POST_X1, POST_Y0, POST_Y1, LEG_ZB, zin + 0.5))
        .union(box(POST_X0, POST_X1, POST_Y0, POST_Y2, POST_ZSTEP, zin + 0.5))
        .union(gus))
body = body.cut(cq.Workplane("XZ", origin=(0, POST_Y0 + POST_PIN_DEPTH, 0)).center(POST_PIN_X, POST_PIN_Z)
                .circle(POST_PIN_D / 2.0).extrude(POST_PIN_DEPTH + 1.0))

# ---------------- snap tabs under the window edges ----------------
for ys in (-1, 1):
    edge_y = WIN_CY + ys * WIN_L / 2.0
    t_in, t_out = TAB_SPANS[ys]
    ty0, ty1 = sorted((edge_y - ys * t_in, edge_y + ys * t_out))
    for xs in (-1, 1):
        x_edge = WIN_CX + xs * WIN_W / 2.0          # tabs hang just outside the opening's side edges
        tx0, tx1 = sorted((x_edge, x_edge + xs * TAB_W))
        tab = box(tx0, tx1, ty0, ty1, zin - TAB_H, zin + 0.2)
        # lead-in slope on the lower edge facing the opening
        tab = tab.edges(cq.selectors.BoxSelector(
            (x_edge - 0.1, ty0 - 1, zin - TAB_H - 0.1), (x_edge + 0.1, ty1 + 1, zin - TAB_H + 0.1))).chamfer(TAB_CH)
        body = body.union(tab)

# ---------------- block behind the key switch ----------------
body = body.union(box(KBLK_X0, KBLK_X1, KBLK_Y0, yw + 0.2, KBLK_ZB, zin + 0.1))

# ---------------- openings through the top plate ----------------
body = body.cut(cq.Workplane("XY", origin=(0, 0, zin - 0.01)).center(WIN_CX, WIN_CY).rect(WIN_W, WIN_L).extrude(T + 1))
body = body.cut(cq.Workplane("XY", origin=(0, 0, zin - 5)).center(0, LED_Y).rect(LED_SQ, LED_SQ).extrude(20))
for dx in (-LED_DX, LED_DX):
    body = body.cut(cq.Workplane("XY", origin=(0, 0, zin - 5)).center(dx, LED_Y).circle(LED_HOLE_D / 2).extrude(20))

# ---------------- key recess + latch slot in the back wall ----------------
y_out_key = L / 2.0 - KEY_Z * tz
body = body.cut(cq.Workplane("XZ", origin=(0, L / 2.0 + 1, 0)).center(KEY_X, KEY_Z)
                .circle(KEY_REC_D / 2).extrude(L / 2.0 + 1 - (y_out_key - KEY_REC_DEPTH)))
body = body.cut(cq.Workplane("XZ", origin=(0, L / 2.0 + 1, 0))
                .center(KEY_X + KEY_SLOT_DX, KEY_Z + KEY_SLOT_DZ)
                .slot2D(KEY_SLOT_L, KEY_SLOT_W).extrude(L / 2.0 + 1 - (yw - 5.0)))

result = body
